import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D_BODY = 60.3          # outer diameter of the cup body
H_BODY = 26.0          # height of the cup body
WALL = 2.3             # side wall thickness
TOP_T = 2.4            # top plate thickness

N_TABS = 6             # mounting tabs around the base
TAB_W = 9.5            # tab width
TAB_T = 2.2            # tab thickness (flush with the bottom)
TAB_TIP_R = 41.7       # radius of the tab tips
TAB_HOLE_D = 4.5       # tab hole diameter
TAB_HOLE_R = 35.9      # radius of the tab hole centres

HEX_AF = 29.6          # hex across flats
HEX_H = 6.0            # hex height

THR_OD = 24.4          # thread major diameter
THR_DEPTH = 1.45       # thread depth
THR_L = 16.9           # threaded length
THR_PITCH = 2.14       # thread pitch
THR_N = 8              # number of thread crests
THR_FIRST = 1.0        # height of the first crest above the hex
BORE_D = 14.6          # bore diameter at the bottom of the top plate (narrowest)
BORE_TOP_D = 17.2      # bore diameter at the top of the spigot (drafted bore)
BORE_FILLET = 1.1      # round at the top inner edge of the spigot
LIP_OUT_R = 0.5        # round at the top outer edge of the spigot
LIP_R_OFF = 0.2        # run-out chamfer ends this far outside the thread root

TUBE_OD = 9.64         # small vent tube (outer side flush with the body wall)
TUBE_ID = 8.3          # bore of the tube
TUBE_STEP_D = 5.7      # step at the bottom of the tube bore
TUBE_HOLE_D = 4.0      # through hole into the cavity
TUBE_H = 11.7          # tube height above the body top
TUBE_FLOOR = 1.0       # height where the tube bore starts to narrow
TUBE_CONE = 60.0       # slope (deg from horizontal) of the narrowing cone
TUBE_FILLET = 2.0      # fillet at the tube base

R = D_BODY / 2.0
R_IN = R - WALL
c45 = math.cos(math.radians(45))


def zrot(wp, deg):
    return wp.rotate((0, 0, 0), (0, 0, 1), deg)


# ---------------- cup body (open at the bottom) ----------------
# cylinders rotated so their seams lie on the back side of the part
body = zrot(cq.Workplane("XY").circle(R).extrude(H_BODY), 135)
cavity = zrot(cq.Workplane("XY").circle(R_IN).extrude(H_BODY - TOP_T), 45)
body = body.cut(cavity)

# ---------------- mounting tabs ----------------
tab_r0 = R - WALL / 2.0
tab_len = TAB_TIP_R - tab_r0
tab = (
    cq.Workplane("XY")
    .box(tab_len, TAB_W, TAB_T, centered=(False, True, False))
    .translate((tab_r0, 0, 0))
)
tab_hole = (
    cq.Workplane("XY")
    .center(TAB_HOLE_R, 0)
    .circle(TAB_HOLE_D / 2.0)
    .extrude(TAB_T)
)
tab = tab.cut(tab_hole)
for i in range(N_TABS):
    body = body.union(zrot(tab, i * 360.0 / N_TABS))

# ---------------- hex ----------------
hex_d = HEX_AF / math.cos(math.radians(30))
hexnut = (
    cq.Workplane("XY")
    .workplane(offset=H_BODY)
    .polygon(6, hex_d)
    .extrude(HEX_H)
)
body = body.union(hexnut)

# drafted through bore: narrowest at the underside of the top plate
z_pb = H_BODY - TOP_T
z0 = H_BODY + HEX_H
zt = z0 + THR_L
r_bore = BORE_D / 2.0
r_btop = BORE_TOP_D / 2.0
tan_b = (r_btop - r_bore) / (zt - z_pb)


def r_at(z):
    """bore radius at height z"""
    return r_bore + (z - z_pb) * tan_b


bore = (
    cq.Workplane("XZ")
    .polyline([(0, z_pb - 1), (r_at(z_pb - 1), z_pb - 1), (r_at(z0), z0), (0, z0)])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(bore)

# ---------------- threaded spigot (revolved ring-thread profile) ----------------
r_maj = THR_OD / 2.0
r_root = r_maj - THR_DEPTH
p = THR_PITCH

pts = [(r_root, z0)]
for k in range(THR_N):
    zc = z0 + THR_FIRST + k * p
    pts += [
        (r_root, zc - 0.45 * p),
        (r_maj, zc - 0.06 * p),
        (r_maj, zc + 0.06 * p),
    ]
    if k < THR_N - 1:
        pts.append((r_root, zc + 0.45 * p))

# rounded lip on top of the spigot: run-out chamfer from the last crest,
# a small outer round, a short flat, and a larger round into the drafted bore
r_o = r_root + LIP_R_OFF                   # outer end of the run-out chamfer
pts.append((r_o, zt - LIP_OUT_R))
c_o = (r_o - LIP_OUT_R, zt - LIP_OUT_R)    # centre of the outer round
m_o = (c_o[0] + LIP_OUT_R * c45, c_o[1] + LIP_OUT_R * c45)
e_o = (r_o - LIP_OUT_R, zt)

beta = math.atan(tan_b)
u1 = (1.0, 0.0)                            # along the top face (outwards)
u2 = (-math.sin(beta), -math.cos(beta))    # down the drafted bore wall
theta = math.acos(u1[0] * u2[0] + u1[1] * u2[1])
t_f = BORE_FILLET / math.tan(theta / 2.0)
bis = (u1[0] + u2[0], u1[1] + u2[1])
nb = math.hypot(*bis)
bis = (bis[0] / nb, bis[1] / nb)
d_c = BORE_FILLET / math.sin(theta / 2.0)
cen = (r_btop + d_c * bis[0], zt + d_c * bis[1])
t1 = (r_btop + t_f * u1[0], zt)
t2 = (r_btop + t_f * u2[0], zt + t_f * u2[1])
mid = (cen[0] - BORE_FILLET * bis[0], cen[1] - BORE_FILLET * bis[1])

prof = cq.Workplane("XZ").moveTo(r_at(z0), z0)
for q in pts:
    prof = prof.lineTo(*q)
prof = (
    prof.threePointArc(m_o, e_o)
    .lineTo(*t1)
    .threePointArc(mid, t2)
    .close()
)
spigot = zrot(prof.revolve(360, (0, 0, 0), (0, 1, 0)), 90)
body = body.union(spigot)

# ---------------- vent tube ----------------
r_t = TUBE_OD / 2.0
ty = -(R - r_t)            # outer side of the tube flush with the body wall


def at_tube(wp):
    """seam on the outer (tangent) side, then move onto the tube axis"""
    return zrot(wp, -90).translate((0, ty, 0))


tube = at_tube(
    cq.Workplane("XY").workplane(offset=H_BODY - 0.5).circle(r_t).extrude(TUBE_H + 0.5)
)

# base fillet: revolved concave ring, trimmed to the body outline
rf = TUBE_FILLET
fil = at_tube(
    cq.Workplane("XZ", origin=(0, 0, H_BODY))
    .moveTo(r_t - 0.05, 0)
    .lineTo(r_t + rf, 0)
    .threePointArc((r_t + rf * (1 - c45), rf * (1 - c45)), (r_t, rf))
    .lineTo(r_t - 0.05, rf)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
trim = cq.Workplane("XY").workplane(offset=H_BODY - 1).circle(R).extrude(rf + 2)
fil = fil.intersect(trim)
body = body.union(tube).union(fil)

# stepped bore of the tube, running through the top plate into the cavity
r_cb = TUBE_ID / 2.0
r_st = TUBE_STEP_D / 2.0
r_h = TUBE_HOLE_D / 2.0
z_fl = H_BODY + TUBE_FLOOR - (r_cb - r_st) * math.tan(math.radians(TUBE_CONE))
ztop = H_BODY + TUBE_H
tube_bore = at_tube(
    cq.Workplane("XZ")
    .polyline([
        (0, H_BODY - TOP_T - 1),
        (r_h, H_BODY - TOP_T - 1),
        (r_h, z_fl),
        (r_st, z_fl),
        (r_cb, H_BODY + TUBE_FLOOR),
        (r_cb, ztop + 1),
        (0, ztop + 1),
    ])
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
body = body.cut(tube_bore)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
